"""Stepped flange ring with a 20-hole pattern counterbored from the underside.

A thin full-diameter flange sits on top of a slightly smaller spigot / step.
A large central bore runs straight through.  Twenty equally spaced holes on a
bolt circle pass through the part; on the underside each hole is opened up by
a deep cylindrical counterbore.
"""
import math
import cadquery as cq

# ---- driving dimensions (mm) ----
OUTER_D = 100.0        # flange outer diameter
FLANGE_T = 3.1         # flange thickness (top)
STEP_D = 85.4          # lower spigot / step diameter
STEP_T = 4.15          # lower step thickness
BORE_D = 43.0          # central through bore
BC_D = 69.0            # bolt circle diameter
HOLE_D = 7.9           # through-hole diameter
N_HOLES = 20           # number of holes (one on +Y, equally spaced)
CBORE_D = 10.0         # counterbore diameter on the underside
CBORE_DEPTH = 3.4      # counterbore depth measured from the underside

# angular position of the cylinder seams (purely cosmetic: at 45 deg the
# seam lines fall on the silhouettes of the oblique views)
OUTER_SEAM_DEG = 45.0
INNER_SEAM_DEG = 45.0

TOTAL_T = FLANGE_T + STEP_T
EPS = 0.01


def cyl(d, h, z0=0.0, seam_deg=0.0, at=(0.0, 0.0)):
    """Cylinder of diameter d, height h starting at z0, seam turned to seam_deg."""
    c = cq.Workplane("XY").workplane(offset=z0).circle(d / 2.0).extrude(h)
    c = c.rotate((0, 0, 0), (0, 0, 1), seam_deg)
    return c.translate((at[0], at[1], 0))


# ---- main body: lower step (z = 0 .. STEP_T) + flange on top ----
step = cyl(STEP_D, STEP_T, 0.0, OUTER_SEAM_DEG)
flange = cyl(OUTER_D, FLANGE_T, STEP_T, OUTER_SEAM_DEG)
body = step.union(flange)

# ---- central bore ----
body = body.cut(cyl(BORE_D, TOTAL_T + 2 * EPS, -EPS, INNER_SEAM_DEG))

# ---- hole pattern: through holes, counterbored from the underside ----
for i in range(N_HOLES):
    a = math.radians(90.0 + i * 360.0 / N_HOLES)
    p = (BC_D / 2.0 * math.cos(a), BC_D / 2.0 * math.sin(a))
    through = cyl(HOLE_D, TOTAL_T + 2 * EPS, -EPS, INNER_SEAM_DEG, p)
    cbore = cyl(CBORE_D, CBORE_DEPTH + EPS, -EPS, INNER_SEAM_DEG, p)
    body = body.cut(through).cut(cbore)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
